import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
# outline of the tray seen from above (X to the right, Y to the back), clockwise
OUTLINE = [
    (0.0, 121.3),    # A  back-left
    (237.9, 121.3),  # B  back-right
    (237.9, 42.1),   # C
    (201.7, 39.9),   # D
    (186.3, 14.4),   # E
    (153.4, 14.4),   # F
    (121.8, 22.8),   # G
    (90.6, 23.1),    # H
    (30.8, -0.8),    # I  front-most point (rounded, its arc touches Y=0)
    (0.0, 54.0),     # J
]
# vertical corner radii of the outline at the top (0 = sharp corner)
CORNER_R = [0.0, 0.0, 3.8, 0.0, 3.5, 3.5, 3.0, 3.0, 3.5, 3.5]
BACK_EDGE = 0            # index of edge A-B (the low back wall)

H_TOTAL = 20.3       # top of the raised lip and the end walls
Z_LEDGE = 13.2       # inner ledge behind the lip
Z_BACK = 7.3         # top of the low back wall
Z_FLOOR = 2.6        # tray floor
CH_H = 10.3          # height of the bevel band round the bottom
CH_IN = 3.1          # inset of that bevel at the bottom face
T_LIP = 2.6          # thickness of the raised lip at its foot
T_END = 3.2          # thickness of the right end wall
Z_STEP = 16.3        # start of the bevel on the inner face of the lip
IN_BEVEL = 0.9       # horizontal size of that inner bevel
W_LEDGE = 1.8        # width of the ledge
TOP_CH = 1.0         # bevel (horizontal) on the outer top edge of the lip
END_CH = 2.0         # bevel on the outer top edge of the right end wall
BEVEL_H = 1.6        # height of those bevels
FLOOR_CH = 3.6       # 45 deg chamfer between inner walls and floor
LEFT_LIP_END_Y = 91.0  # the raised lip on the left end stops here

BOSS_D = 9.0
BOSS_TOP = 9.2
BOSS_HOLE_D = 4.5
BOSS_BASE_R = 1.0
BOSS_TOP_CH = 0.5
BOSS_HOLE_CH = 0.6
BOSSES = [(31.4, 56.9), (73.1, 85.9), (201.6, 82.0)]

VIEW = {"azimuth": 45, "elevation": 26}

X_MAX = max(p[0] for p in OUTLINE)
Y_MAX = max(p[1] for p in OUTLINE)
N = len(OUTLINE)


# ---------------- 2D helpers ----------------
def convex_flags(pts):
    n = len(pts)
    flags = []
    for i in range(n):
        ax, ay = pts[i - 1]
        bx, by = pts[i]
        cx, cy = pts[(i + 1) % n]
        cross = (bx - ax) * (cy - by) - (by - ay) * (cx - bx)
        flags.append(cross < 0)          # clockwise polygon -> convex if cross < 0
    return flags


CONVEX = convex_flags(OUTLINE)


def offset_poly(pts, dists):
    """Offset every edge of a clockwise polygon inwards by its own distance
    (negative = outwards) and return the new sharp corner points."""
    n = len(pts)
    lines = []
    for i in range(n):
        x0, y0 = pts[i]
        x1, y1 = pts[(i + 1) % n]
        dx, dy = x1 - x0, y1 - y0
        ln = math.hypot(dx, dy)
        nx, ny = dy / ln, -dx / ln          # inward normal for clockwise order
        d = dists[i]
        lines.append(((x0 + nx * d, y0 + ny * d), (dx / ln, dy / ln)))
    out = []
    for i in range(n):
        (p, u) = lines[i - 1]
        (q, v) = lines[i]
        den = u[0] * v[1] - u[1] * v[0]
        t = ((q[0] - p[0]) * v[1] - (q[1] - p[1]) * v[0]) / den
        out.append((p[0] + u[0] * t, p[1] + u[1] * t))
    return out


def offset_radii(d, min_r=0.0):
    """corner radii after an inward offset d of the outline"""
    out = []
    for r, cv in zip(CORNER_R, CONVEX):
        if r <= 0:
            out.append(0.0)
        elif cv:
            out.append(max(r - d, min_r))
        else:
            out.append(r + d)
    return out


def rounded_wire(pts, radii, z):
    """closed wire through pts (sharp polygon) with tangent arcs of the given radii"""
    n = len(pts)
    segs = []   # per vertex: (entry point, arc mid or None, exit point)
    for i in range(n):
        px, py = pts[i - 1]
        vx, vy = pts[i]
        qx, qy = pts[(i + 1) % n]
        r = radii[i]
        if r <= 1e-6:
            segs.append(((vx, vy), None, (vx, vy)))
            continue
        ux, uy = vx - px, vy - py
        lu = math.hypot(ux, uy)
        ux, uy = ux / lu, uy / lu
        wx, wy = qx - vx, qy - vy
        lw = math.hypot(wx, wy)
        wx, wy = wx / lw, wy / lw
        cosphi = -(ux * wx + uy * wy)            # angle between the two edges at the vertex
        phi = math.acos(max(-1.0, min(1.0, cosphi)))
        t = r / math.tan(phi / 2)
        t1 = (vx - ux * t, vy - uy * t)
        t2 = (vx + wx * t, vy + wy * t)
        bx, by = -ux + wx, -uy + wy
        lb = math.hypot(bx, by)
        bx, by = bx / lb, by / lb
        dm = r / math.sin(phi / 2) - r
        mid = (vx + bx * dm, vy + by * dm)
        segs.append((t1, mid, t2))
    edges = []
    V = lambda p: cq.Vector(p[0], p[1], z)
    for i in range(n):
        t1, mid, t2 = segs[i]
        if mid is not None:
            edges.append(cq.Edge.makeThreePointArc(V(t1), V(mid), V(t2)))
        nxt = segs[(i + 1) % n][0]
        edges.append(cq.Edge.makeLine(V(t2), V(nxt)))
    return cq.Wire.assembleEdges(edges)


def prism(wire, z0, z1):
    face = cq.Face.makeFromWires(wire)
    return cq.Workplane("XY").add(
        cq.Solid.extrudeLinear(face, cq.Vector(0, 0, z1 - z0))
    )


def wire_at(d_edges, d_corner, z, min_r=0.0, radii=None):
    pts = offset_poly(OUTLINE, d_edges)
    if radii is None:
        radii = offset_radii(d_corner, min_r)
    return rounded_wire(pts, radii, z)


# ---------------- outer body ----------------
foot_d = [CH_IN] * N
foot_d[BACK_EDGE] = 0.0                      # the back face runs straight down
w_foot = wire_at(foot_d, CH_IN, 0.0)
w_mid = wire_at([0.0] * N, 0.0, CH_H)
w_sh = wire_at([0.0] * N, 0.0, H_TOTAL - BEVEL_H)
top_d = [TOP_CH] * N
top_d[1] = END_CH                            # edge B-C: right end wall
w_top = wire_at(top_d, TOP_CH, H_TOTAL)

lower = cq.Solid.makeLoft([w_foot, w_mid], True)
wall = cq.Solid.extrudeLinear(cq.Face.makeFromWires(w_mid), cq.Vector(0, 0, H_TOTAL - BEVEL_H - CH_H))
crown = cq.Solid.makeLoft([w_sh, w_top], True)
body = cq.Workplane("XY").add(lower).union(cq.Workplane("XY").add(wall)).union(
    cq.Workplane("XY").add(crown))

# ---------------- lip: cut the inside down to the ledge ----------------
lip_d = [T_LIP] * N
lip_d[1] = T_END                             # right end wall is a bit thicker
lip_d[BACK_EDGE] = -10.0                     # no lip along the back
lip_cut = prism(wire_at(lip_d, T_LIP, Z_LEDGE, min_r=1.5), Z_LEDGE, Z_STEP)
# inner bevel: the lip gets thinner towards its top
z_hi = H_TOTAL + 1.0
k = IN_BEVEL * (z_hi - Z_STEP) / (H_TOTAL - Z_STEP)
lip_d_hi = [d - k if d > 0 else d for d in lip_d]
lip_bevel = cq.Solid.makeLoft(
    [wire_at(lip_d, T_LIP, Z_STEP, min_r=1.5), wire_at(lip_d_hi, T_LIP - k, z_hi, min_r=1.5 + k)],
    True,
)
body = body.cut(lip_cut).cut(cq.Workplane("XY").add(lip_bevel))
# rear part of the left end is cut down to the ledge as well
body = body.cut(
    cq.Workplane("XY")
    .box(T_LIP + 10, Y_MAX - LEFT_LIP_END_Y + 10, H_TOTAL, centered=False)
    .translate((-10, LEFT_LIP_END_Y, Z_LEDGE))
)

# ---------------- low back wall ----------------
inner = T_LIP + W_LEDGE
body = body.cut(
    cq.Workplane("XY")
    .box(X_MAX - 2 * inner, inner + 10, H_TOTAL, centered=False)
    .translate((inner, Y_MAX - inner - 0.01, Z_BACK))
)

# ---------------- rounded ends of the raised walls ----------------
def round_tool(axis, a0, a1, c1, c2, r, s1, s2):
    """Solid that rounds a straight convex edge running along `axis` ('X' or 'Y')
    from a0 to a1.  (c1, c2) is the edge position in the two other coordinates
    (Y,Z for an X edge; X,Z for a Y edge); s1, s2 = +-1 point away from the material."""
    ln = a1 - a0
    sq = cq.Workplane("XY").box(ln, r, r, centered=False)
    cyl = cq.Workplane("YZ").circle(r).extrude(ln)
    # build in a local frame: length along X, width along Y, height along Z
    sq = sq.translate((0, -r if s1 > 0 else 0, -r if s2 > 0 else 0))
    cyl = cyl.translate((0, -r * s1, -r * s2))
    tool = sq.cut(cyl)
    if axis == "X":
        return tool.translate((a0, c1, c2))
    tool = tool.rotate((0, 0, 0), (0, 0, 1), 90)      # local X -> global Y, local Y -> -X
    tool = tool.mirror("YZ")                           # local Y -> +X
    return tool.translate((c1, a0, c2))


FIN_END_R = 3.0      # rounding of the end of the left raised lip
REAR_WALL_R = 1.6    # rounding of the back corner of the rear-left wall
END_WALL_R = 2.0     # rounding of the back top corner of the right end wall
BACK_TOP_R = 0.8     # small round on the top outer edge of the back wall

body = body.cut(round_tool("X", -1, T_LIP + 1, LEFT_LIP_END_Y, H_TOTAL, FIN_END_R, 1, 1))
body = body.cut(round_tool("X", -1, inner + 0.01, Y_MAX, Z_LEDGE, REAR_WALL_R, 1, 1))
body = body.cut(round_tool("X", X_MAX - inner - 0.01, X_MAX + 1, Y_MAX, H_TOTAL, END_WALL_R, 1, 1))
body = body.cut(round_tool("X", inner, X_MAX - inner, Y_MAX, Z_BACK, BACK_TOP_R, 1, 1))
body = body.cut(round_tool("Y", LEFT_LIP_END_Y, Y_MAX + 1, 0.0, Z_LEDGE, REAR_WALL_R, -1, 1))

# ---------------- tray pocket ----------------
pk_radii = offset_radii(inner, min_r=FLOOR_CH + 0.6)
pk_radii[3] = FLOOR_CH + 0.6                 # soften the inner corner at D
pocket = prism(wire_at([inner] * N, inner, Z_FLOOR, radii=pk_radii), Z_FLOOR, H_TOTAL + 1)
pocket = pocket.faces("<Z").edges().chamfer(FLOOR_CH)
body = body.cut(pocket)

# ---------------- bosses ----------------
for (bx, by) in BOSSES:
    boss = (
        cq.Workplane("XY").workplane(offset=Z_FLOOR - 0.5)
        .center(bx, by).circle(BOSS_D / 2).extrude(BOSS_TOP - Z_FLOOR + 0.5)
        .faces(">Z").edges().chamfer(BOSS_TOP_CH)
    )
    body = body.union(boss)
    try:
        body = body.edges(
            cq.selectors.BoxSelector((bx - BOSS_D, by - BOSS_D, Z_FLOOR - 0.05),
                                     (bx + BOSS_D, by + BOSS_D, Z_FLOOR + 0.05))
        ).fillet(BOSS_BASE_R)
    except Exception:
        pass
for (bx, by) in BOSSES:
    hole = (
        cq.Workplane("XY").workplane(offset=Z_FLOOR)
        .center(bx, by).circle(BOSS_HOLE_D / 2).extrude(BOSS_TOP)
    )
    body = body.cut(hole)
    try:
        body = body.edges(
            cq.selectors.BoxSelector((bx - BOSS_HOLE_D, by - BOSS_HOLE_D, BOSS_TOP - 0.05),
                                     (bx + BOSS_HOLE_D, by + BOSS_HOLE_D, BOSS_TOP + 0.05))
        ).edges(cq.selectors.RadiusNthSelector(0)).chamfer(BOSS_HOLE_CH)
    except Exception:
        pass

result = body
